import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_F = 30.0          # bead flange outer radius
R_B = 27.9          # barrel outer radius
R_I = 25.5          # barrel bore radius
L = 30.8            # overall width (along X, wheel axis)
T_F = 2.4           # bead flange axial thickness
BEAD_OUT = 0.75     # small round on the outside of the bead
BEAD_IN = 1.6       # large round on the tyre side of the bead
LIP_RAD = 2.6       # conical flare where the bore opens to the front face (radial size)
LIP_AX = 4.7        # ... and its axial length
LIP_BLEND = 1.2     # extra length over which the flare blends into the bore

EDGE_DEPTH = 8.7    # depth of the hub-disc rim below the front face
SPOKE_END_DEPTH = 4.2  # spokes rise toward the rim: depth of their top at the bore
R_D = 18.7          # hub disc radius (inner edge of the openings)
CROWN = 2.2         # the hub face is a shallow cone rising toward the centre
BOSS_R = 6.7        # raised ring around the axle hole
BOSS_H = 1.0
HOLE_R = 3.4        # axle hole
HOLE_CH = 0.75

SPOKE_ANGLES = (90.0, 210.0, 330.0)   # degrees in the Y-Z plane
SPOKE_W = 3.5       # spoke width at the neck
CORNER_IN = 2.6     # opening corner radius at the hub
CORNER_OUT = 2.3    # opening corner radius at the barrel
GAP_EDGE_F = 1.1    # front edge round of the openings

NOTCH_R0 = 10.8     # inner radius of the three back notches (open into the openings)
NOTCH_W = 5.2
NOTCH_DEPTH = 9.5
PIN_R = 2.3         # drive pin standing in one notch
PIN_HOLE_R = 0.9
PIN_RAD = 13.3      # radial position of the drive pin
PIN_ANGLE = 30.0
V_HALF = 4.8        # V notches in the back rim at the middle of each opening: half mouth width
V_LEN = 3.0         # how far the mouth reaches into the rim face
V_DEPTH = 4.5       # depth of the notch at the bore
BACK_CH = 0.5       # chamfer on the back end of the axle hole

X0 = -L / 2.0
X1 = L / 2.0
X_E = X1 - EDGE_DEPTH            # spoke top / disc rim plane
X_C = X_E + CROWN                # cone height at the boss
X_S = X1 - SPOKE_END_DEPTH       # spoke top at the bore
K_S = (X_S - X_E) / (R_I - R_D)  # axial rise of the spoke top per mm of radius

C45 = math.cos(math.radians(45.0))


SEAM_ANGLE = 330.0  # park the seams of the revolved faces under a spoke


def polar(r, ang_deg):
    a = math.radians(ang_deg)
    return r * math.cos(a), r * math.sin(a)


def revolve_x(wp, seam=SEAM_ANGLE):
    sol = wp.revolve(360.0, (0, 0, 0), (1, 0, 0)).val()
    return sol.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), seam)


# ---------------- barrel with the two bead flanges ----------------
# profile in the X-Y plane (x = axial, y = radius), revolved about X
a, b = BEAD_OUT, BEAD_IN
barrel_wp = (
    cq.Workplane("XY")
    .moveTo(X0, R_I)
    .lineTo(X0, R_F - a)
    .threePointArc((X0 + a - a * C45, R_F - a + a * C45), (X0 + a, R_F))
    .threePointArc((X0 + a + b * C45, R_F - b + b * C45), (X0 + a + b, R_F - b))
    .lineTo(X0 + T_F, R_B)
    .lineTo(X1 - T_F, R_B)
    .lineTo(X1 - a - b, R_F - b)
    .threePointArc((X1 - a - b * C45, R_F - b + b * C45), (X1 - a, R_F))
    .threePointArc((X1 - a + a * C45, R_F - a + a * C45), (X1, R_F - a))
    .lineTo(X1, R_I)
    .close()
)
barrel = revolve_x(barrel_wp)

# ---------------- hub: crowned disc, axle boss and bore ----------------
hub_wp = (
    cq.Workplane("XY")
    .moveTo(X0 + BACK_CH, HOLE_R)
    .lineTo(X0, HOLE_R + BACK_CH)
    .lineTo(X0, R_D)
    .lineTo(X_E, R_D)
    .lineTo(X_C, BOSS_R)
    .lineTo(X_C + BOSS_H, BOSS_R)
    .lineTo(X_C + BOSS_H, HOLE_R + HOLE_CH)
    .lineTo(X_C + BOSS_H - HOLE_CH, HOLE_R)
    .close()
)
hub = revolve_x(hub_wp)


# ---------------- spoke ring: three spokes joining hub and barrel ----------------
def yz_prism(sketch, x_from, x_to):
    return (
        cq.Workplane("YZ", origin=(x_from, 0, 0))
        .placeSketch(sketch)
        .extrude(x_to - x_from)
        .val()
    )


ring_in = R_D - 2.5
ring_out = R_I + 0.1


def on_cone(p, tol=1e-3):
    r = math.hypot(p.y, p.z)
    return abs(p.x - (X_E + (r - R_D) * K_S)) < tol


def good(shape):
    return shape is not None and shape.isValid() and len(shape.Solids()) == 1


def build_spoke_ring(edge_round):
    ring = yz_prism(cq.Sketch().circle(ring_out).circle(ring_in, mode="s"), X0, X1 - 0.3)
    # conical top: the spokes climb from the hub rim toward the front of the barrel
    x_in = X_E + (ring_in - 1.0 - R_D) * K_S
    x_out = X_E + (ring_out + 1.0 - R_D) * K_S
    cone_cut = revolve_x(
        cq.Workplane("XY")
        .moveTo(x_in, ring_in - 1.0)
        .lineTo(x_out, ring_out + 1.0)
        .lineTo(X1 + 5.0, ring_out + 1.0)
        .lineTo(X1 + 5.0, ring_in - 1.0)
        .close(),
        seam=0.0,    # seam inside an opening
    )
    ring = ring.cut(cone_cut)

    # the three openings: annulus minus the three spoke strips
    gap_sk = cq.Sketch().circle(R_I + 0.05).circle(R_D - 0.05, mode="s")
    for ang in SPOKE_ANGLES:
        cx, cy = polar(R_F, ang)
        gap_sk = gap_sk.push([(cx, cy)]).rect(2.0 * R_F, SPOKE_W, angle=ang, mode="s").reset()
    ring = ring.cut(yz_prism(gap_sk, X0 - 1.0, X1 + 1.0))

    # round the axial corner edges of the openings (U shaped ends)
    e_in, e_out = [], []
    for e in ring.Edges():
        if e.geomType() != "LINE":
            continue
        p0, p1 = e.startPoint(), e.endPoint()
        if abs(p0.y - p1.y) > 1e-6 or abs(p0.z - p1.z) > 1e-6:
            continue  # not parallel to X
        rr = math.hypot(p0.y, p0.z)
        if abs(rr - R_I) < 1.0:
            e_out.append(e)
        elif abs(rr - R_D) < 1.0:
            e_in.append(e)
    ring = ring.fillet(CORNER_IN, e_in)
    ring = ring.fillet(CORNER_OUT, e_out)

    # round the front edges of the openings (closed loops on the conical top)
    if edge_round > 0:
        top = []
        for e in ring.Edges():
            pts = [e.positionAt(t) for t in (0.0, 0.37, 0.73, 1.0)]
            if not all(on_cone(p) for p in pts):
                continue
            rr = [math.hypot(p.y, p.z) for p in pts]
            if max(rr) - min(rr) < 1e-3 and (abs(rr[0] - ring_out) < 1e-3 or abs(rr[0] - ring_in) < 1e-3):
                continue
            top.append(e)
        try:
            rounded = ring.fillet(edge_round, top)
            if good(rounded):
                ring = rounded
        except Exception:
            pass
    return ring


def build_front(edge_round):
    ring = build_spoke_ring(edge_round)
    body = cq.Workplane("XY").add(barrel).union(hub).union(ring)
    # the front flare of the bore is cut after the union so the spokes run cleanly
    # into it; it is conical and blends smoothly into the bore
    flare = revolve_x(
        cq.Workplane("XY")
        .moveTo(X1, R_I + LIP_RAD)
        .spline([(X1 - LIP_AX - LIP_BLEND, R_I)], tangents=[(-LIP_AX, -LIP_RAD), (-1.0, 0.0)],
                includeCurrent=True)
        .lineTo(X1 + 0.5, R_I)
        .lineTo(X1 + 0.5, R_I + LIP_RAD + 0.3)
        .close()
    )
    return body.cut(flare)


body = None
for er in (GAP_EDGE_F, 0.8 * GAP_EDGE_F, 0.0):
    try:
        cand = build_front(er)
        if good(cand.val()):
            body = cand
            break
    except Exception:
        continue
if body is None:                      # last resort: plain spokes, no edge rounding
    body = build_front(0.0)


# ---------------- back face details ----------------
gap_mids = [a + 60.0 for a in SPOKE_ANGLES]   # 150, 270, 30 degrees

# rectangular notches running inward from each opening
notch_len = (R_D + 1.0) - NOTCH_R0
for gm in gap_mids:
    cx, cy = polar(NOTCH_R0 + 0.5 * notch_len, gm)
    nt = (
        cq.Workplane("YZ", origin=(X0 - 1.0, 0, 0))
        .center(cx, cy)
        .transformed(rotate=(0, 0, gm))
        .rect(notch_len, NOTCH_W)
        .extrude(NOTCH_DEPTH + 1.0)
    )
    body = body.cut(nt)

# drive pin with a small bore, standing in the notch at PIN_ANGLE
px, py = polar(PIN_RAD, PIN_ANGLE)
pin = (
    cq.Workplane("YZ", origin=(X0 + 0.3, 0, 0))
    .center(px, py)
    .circle(PIN_R)
    .circle(PIN_HOLE_R)
    .extrude(NOTCH_DEPTH + 0.5)
)
body = body.union(pin)


# small V shaped notches in the back rim at the middle of each opening:
# a tetrahedron with its deepest point on the bore and a triangular mouth on the back face
def v_cut(ang):
    V = cq.Vector
    r_in = R_I - 0.5
    dang = math.degrees(V_HALF / R_I)
    deep = V(X0 + V_DEPTH, *polar(r_in, ang))
    mouth = [V(X0, *polar(R_I + V_LEN, ang)),
             V(X0, *polar(r_in, ang - dang)),
             V(X0, *polar(r_in, ang + dang))]
    f = (V_DEPTH + 1.0) / V_DEPTH        # extend the mouth 1 mm behind the back face
    base = [deep + (m - deep) * f for m in mouth]
    faces = [
        cq.Face.makeFromWires(cq.Wire.makePolygon([base[0], base[1], base[2]], close=True)),
        cq.Face.makeFromWires(cq.Wire.makePolygon([base[0], base[1], deep], close=True)),
        cq.Face.makeFromWires(cq.Wire.makePolygon([base[1], base[2], deep], close=True)),
        cq.Face.makeFromWires(cq.Wire.makePolygon([base[2], base[0], deep], close=True)),
    ]
    sol = cq.Solid.makeSolid(cq.Shell.makeShell(faces))
    if sol.Volume() < 0:
        sol = cq.Solid(sol.wrapped.Reversed())
    return sol


for gm in gap_mids:
    body = body.cut(cq.Workplane("XY").add(v_cut(gm)))

result = body
VIEW = {"azimuth": 45, "elevation": 26}
